"""Square mounting plate with tilted corner chamfers, four octagonal bosses on top,
countersunk / tapered holes opening on the underside and four shallow underside recesses."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 240.0                   # plate width (square)
T = 6.0                     # plate thickness
C_TOP = 24.8                # corner chamfer leg measured on the top face
CORNER_TILT = 45.0          # corner faces lean outward-down by this angle from vertical
C_DROP = math.sqrt(2.0) * T * math.tan(math.radians(CORNER_TILT))  # extra leg at the bottom face

SMALL_D = 5.5               # small through holes (top face)
SMALL_CSK_D = 12.6          # countersink diameter on the underside
CSK_ANGLE = 120.0           # included angle of the countersink
LARGE_D = 9.2               # large holes, diameter at the top face
LARGE_BOT_D = 13.0          # large holes taper out to this diameter on the underside

BOSS_F = 17.0               # octagonal boss: across flats
BOSS_E = 4.5                # octagonal boss: corner chamfer of the square
BOSS_H = 4.8                # boss height above the plate
BOSS_HOLE = 8.5             # bore through boss and plate

REC_D = 16.4                # shallow circular recesses on the underside
REC_DEPTH = 0.6

# ---------------- feature layout (x, y), origin = plate centre, +Y = back edge ----------------
EDGE_X_SMALL = 107.3        # small holes along the left/right edges
EDGE_X_SMALL_2 = 106.4      # the upper small hole of each side column
EDGE_X_LARGE = 108.3        # large holes along the left/right edges
BOSS_X = 58.0
BOSS_Y = (42.3, -20.8)

side_small = [(EDGE_X_SMALL_2, 30.9), (EDGE_X_SMALL, -50.4), (EDGE_X_SMALL, -75.4)]
small_pts = (
    [(-73.3, 103.8), (-51.0, 103.8), (73.3, 103.8), (51.0, 65.3)]        # back row + one inner hole
    + [(x, y) for (x, y) in side_small] + [(-x, y) for (x, y) in side_small]
)
large_pts = [(sx * EDGE_X_LARGE, y) for sx in (-1, 1) for y in (70.4, -20.8)]
boss_pts = [(sx * BOSS_X, y) for sx in (-1, 1) for y in BOSS_Y]
rec_pts = [(sx * 74.3, y) for sx in (-1, 1) for y in (79.4, -93.8)]

# ---------------- plate with tilted corner chamfers ----------------
a = W / 2.0
plate = cq.Workplane("XY").rect(W, W).extrude(T)

c_bot = C_TOP + C_DROP      # chamfer leg at the bottom face
big = 4 * W
for sx, sy in [(1, 1), (-1, 1), (-1, -1), (1, -1)]:
    # half-space beyond the tilted corner plane (passes through the top and bottom chamfer lines)
    n = cq.Vector(sx, sy, -C_DROP / T).normalized()
    origin = cq.Vector(sx * (a - c_bot / 2.0), sy * (a - c_bot / 2.0), 0.0)
    xdir = cq.Vector(-sy, sx, 0.0).normalized()
    cutter = cq.Workplane(cq.Plane(origin=origin, xDir=xdir, normal=n)).rect(big, big).extrude(big)
    plate = plate.cut(cutter)

# ---------------- octagonal bosses on the top face ----------------
bosses = (
    cq.Workplane("XY").workplane(offset=T)
    .pushPoints(boss_pts)
    .rect(BOSS_F, BOSS_F)
    .extrude(BOSS_H)
    .edges("|Z").chamfer(BOSS_E)
)
plate = plate.union(bosses)

# bores straight through boss and plate
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(boss_pts).circle(BOSS_HOLE / 2.0).extrude(T + BOSS_H + 2.0)
)

# ---------------- small holes: countersunk from the underside ----------------
half = math.radians(CSK_ANGLE / 2.0)
for (x, y) in small_pts:
    bore = cq.Workplane("XY").workplane(offset=-1.0).center(x, y).circle(SMALL_D / 2.0).extrude(T + 2.0)
    r0 = SMALL_CSK_D / 2.0 + 1.0 * math.tan(half)          # cone starts 1 mm below the underside
    csk = cq.Solid.makeCone(r0, 0.0, r0 / math.tan(half), pnt=cq.Vector(x, y, -1.0), dir=cq.Vector(0, 0, 1))
    plate = plate.cut(bore.union(cq.Workplane("XY").add(csk)))

# ---------------- large holes: conical, widening towards the underside ----------------
slope = (LARGE_BOT_D - LARGE_D) / (2.0 * T)                 # radius change per mm of depth
for (x, y) in large_pts:
    taper = cq.Solid.makeCone(LARGE_BOT_D / 2.0 + 0.5 * slope, LARGE_D / 2.0 - 0.5 * slope, T + 1.0,
                              pnt=cq.Vector(x, y, -0.5), dir=cq.Vector(0, 0, 1))
    plate = plate.cut(cq.Workplane("XY").add(taper))

# ---------------- shallow recesses on the underside ----------------
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(rec_pts).circle(REC_D / 2.0).extrude(1.0 + REC_DEPTH)
)

result = plate
